import math
import cadquery as cq

# =====================================================================
#  Gear-drive housing with drum, raised cover and splined plug shaft
#  Y = length (shaft points +Y), Z = up, X = thickness (cover on +X)
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
L = 100.0          # body length along Y
H = 64.0           # body height along Z
R_END = 24.6       # radius of the rounded gear end (-Y)
CY, CZ = R_END, H - R_END   # gear / drum centre in the Y-Z plane
R_TR = 22.0        # top-right corner radius of the outline
R_BR = 26.0        # bottom-right corner radius
R_BL = 10.0        # fillet between bottom edge and the diagonal
DIAG = 36.3        # angle of the bottom-left diagonal (deg)

DOME_R = 87.0      # radius of the slightly curved back (-X) face
DOME_ZC = 33.5     # height of the crown of the back face
DOME_CH_FACE = 9.0 # back-face perimeter chamfer: length on the back face
DOME_CH_SIDE = 5.8 #   ... and on the side walls
DOME_BLEND = 6.0   # round between chamfer and back face
END_CH_X = 12.0    # conical chamfer on the gear end (-Y): length along X
END_CH_R = 8.8     #   ... and radial depth
X_RIM = 21.7       # housing front (rim) face
X_FLOOR = 17.0     # floor of the drum pocket
X_DRUM = 29.5      # drum face
X_COVER = 37.4     # cover face (overall thickness)

RIM_EDGE = 0.8     # small round on the rim lip

R_POCKET = 21.0    # drum pocket radius
R_DRUM = 17.5      # drum radius
DRUM_CHAMFER = 0.6
N_BOLTS = 12       # bolts on the drum face
R_BOLTS = 15.0
BOLT_AF = 2.4      # across-corners of the bolt hex heads
HEX_PLATE = 13.0   # central hex plate (across corners)
HEX_PLATE_T = 1.4
HEX_NUT = 5.2      # central nut (across corners)
HEX_NUT_T = 1.4
BORE_R = 1.2
SLOT2_X = 19.0     # strap slot in the diagonal face: centre X, Z, length, width, depth
SLOT2_Z = 4.2
SLOT2_LEN = 4.6
SLOT2_W = 1.8
SLOT2_DEPTH = 5.0

COVER_RA = 20.0        # convex blend radius, top-left of cover outline
COVER_RB = 10.6        # convex blend radius, bottom-left of cover outline
COVER_EDGE_BIG = 4.0   # round on the side of the cover facing the drum
COVER_EDGE_SIDE = 13.0 # round on the +Y end of the cover
COVER_EDGE_SMALL = 2.0 # crisp edge on top / bottom
COVER_EDGE_BL = 3.5    # round at the bottom-left corner
COVER_EDGE_ARCB = 3.5  # round on the lower blend arc
COVER_HOLE_R = 1.3
COVER_HOLES = [(85.1, 54.9), (90.0, 24.5), (67.5, 4.8)]
RIM_SCREWS = [(35.3, 58.3), (22.6, 14.5)]

SHAFT_X = 15.3     # shaft axis position (X) ; Z = CZ
SHAFT_R = 7.0      # core radius of the plug
RIB_R = 7.7        # outer radius of the barb rings
N_RIBS = 7
RIB_PITCH = 4.6
RIB_W = 2.2
SHAFT_LEN = 41.6   # protrusion beyond the housing
COLLAR_LEN = 10.3  # smooth part next to the housing
SHAFT_BORE = 3.6
SLOT_W = 1.6
SLOT_Y0 = 119.0    # split slot extent along Y
SLOT_Y1 = 139.5


def _on(c, r, ang):
    return (c[0] + r * math.cos(math.radians(ang)), c[1] + r * math.sin(math.radians(ang)))


def yz(x):
    return cq.Workplane("YZ", origin=(x, 0, 0))


def _diag():
    a = math.radians(DIAG)
    n = (-math.sin(a), -math.cos(a))                 # outward normal of the diagonal
    nang = math.degrees(math.atan2(n[1], n[0]))      # ~ -126 deg
    fy = CY + (R_END - R_BL - (R_BL - CZ) * n[1]) / n[0]
    return n, nang, (fy, R_BL)


def pear(wp):
    """Housing outline in the Y-Z plane: gear circle at -Y, straight top, rounded
    +Y end, straight bottom and a diagonal chamfer below the gear."""
    n, nang, F = _diag()
    tr = (L - R_TR, H - R_TR)
    br = (L - R_BR, R_BR)
    return (wp.moveTo(CY, H).lineTo(tr[0], H)
            .threePointArc(_on(tr, R_TR, 45), (L, tr[1])).lineTo(L, br[1])
            .threePointArc(_on(br, R_BR, -45), (br[0], 0)).lineTo(F[0], 0)
            .threePointArc(_on(F, R_BL, (-90 + nang) / 2.0), _on(F, R_BL, nang))
            .lineTo(*_on((CY, CZ), R_END, nang))
            .threePointArc(_on((CY, CZ), R_END, (nang + 360 + 90) / 2.0), (CY, H))
            .close())


def variable_fillet(wp, seed_edge, radius_at):
    """Fillet the G1 edge chain through seed_edge with a radius that varies linearly
    along each edge between radius_at(start) and radius_at(end)."""
    from OCP.BRepFilletAPI import BRepFilletAPI_MakeFillet
    mf = BRepFilletAPI_MakeFillet(wp.val().wrapped)
    mf.Add(seed_edge.wrapped)
    for ic in range(1, mf.NbContours() + 1):
        ne = mf.NbEdges(ic)
        edges = [cq.Edge(mf.Edge(ic, ie)) for ie in range(1, ne + 1)]
        for ie, e in enumerate(edges):
            p0, p1 = e.startPoint(), e.endPoint()
            r0, r1 = radius_at(p0), radius_at(p1)
            if abs(r0 - r1) < 1e-6:
                mf.SetRadius(r0, ic, ie + 1)
                continue
            nxt = edges[(ie + 1) % ne]
            qs = [nxt.startPoint(), nxt.endPoint()]
            d0 = min((p0 - q).Length for q in qs)
            d1 = min((p1 - q).Length for q in qs)
            if d1 <= d0:        # traversal runs p0 -> p1
                mf.SetRadius(r0, r1, ic, ie + 1)
            else:
                mf.SetRadius(r1, r0, ic, ie + 1)
    mf.Build()
    if not mf.IsDone():
        raise RuntimeError("fillet failed")
    return cq.Workplane("XY").newObject([cq.Shape.cast(mf.Shape())])


# ---------------- back housing with cushion dome (-X side) ----------------
# the -X face is a large-radius cylinder (axis along Y); its whole perimeter is
# chamfered (asymmetric: long on the face, short on the side walls)
back = pear(yz(0)).extrude(X_RIM)
dome_cyl = (cq.Workplane("XZ", origin=(0, L + 5, 0))
            .center(DOME_R, DOME_ZC).circle(DOME_R).extrude(L + 10))
back = back.intersect(dome_cyl)


def dome_chamfer(wp, d_face, d_side):
    from OCP.BRepFilletAPI import BRepFilletAPI_MakeChamfer
    face = wp.faces("<X").val()
    mc = BRepFilletAPI_MakeChamfer(wp.val().wrapped)
    mc.Add(d_face, d_side, face.Edges()[0].wrapped, face.wrapped)
    mc.Build()
    shp = cq.Shape.cast(mc.Shape())
    if not mc.IsDone() or not shp.isValid():
        raise RuntimeError("chamfer failed")
    return cq.Workplane("XY").newObject([shp])


try:
    back = dome_chamfer(back, DOME_CH_FACE, DOME_CH_SIDE)
    back = back.faces("<X").edges().fillet(DOME_BLEND)     # soften chamfer / back-face crease
except Exception:
    back = back.faces("<X").edges().fillet(4.0)

# the rounded gear end (-Y) gets a deeper, conical chamfer toward the back face
# (revolved around the gear axis over the circular part of the outline, then
#  continued as a prism along the diagonal so it fades into the regular chamfer)
_n, _nang, _F = _diag()
_prof = [(-1, R_END - END_CH_R - END_CH_R / END_CH_X), (END_CH_X, R_END),
         (END_CH_X, R_END + 6), (-1, R_END + 6)]
_pl = cq.Plane(origin=(0, CY, CZ), xDir=(1, 0, 0), normal=(0, -1, 0))
_cone = cq.Workplane(_pl).polyline(_prof).close().revolve((_nang + 360.0) - 90.0, (0, 0, 0), (1, 0, 0))
_d = (0.0, -_n[1], _n[0])                     # direction of the diagonal (downwards, +Y)
_t1 = (CY + R_END * _n[0], CZ + R_END * _n[1])
_t2 = (_F[0] + R_BL * _n[0], _F[1] + R_BL * _n[1])
_len = (_t2[0] - _t1[0]) * _d[1] + (_t2[1] - _t1[1]) * _d[2]
_pl2 = cq.Plane(origin=(0, CY, CZ), xDir=(1, 0, 0), normal=_d)
_prism = cq.Workplane(_pl2).polyline(_prof).close().extrude(_len)
back = back.cut(_cone.union(_prism))

# small round on the outer edge of the rim face
try:
    back = back.faces(">X").edges().fillet(RIM_EDGE)
except Exception:
    pass

# drum pocket sunk into the rim face, leaving a thin lip around the gear end
pocket = yz(X_FLOOR).center(CY, CZ).circle(R_POCKET).extrude(X_RIM - X_FLOOR + 0.01)
back = back.cut(pocket)


# ---------------- raised cover on the +X side ----------------
def cover_geometry():
    """Cover outline (Y-Z): the outer part follows the housing outline; the inner side
    wraps the drum pocket with a concave arc blended by two convex arcs (A at the top
    tangent to the top edge, B at the bottom-left tangent to the diagonal)."""
    n, nang, F = _diag()
    tr = (L - R_TR, H - R_TR)
    br = (L - R_BR, R_BR)
    ra, rb = COVER_RA, COVER_RB
    A = (CY + math.sqrt((ra + R_POCKET) ** 2 - (H - ra - CZ) ** 2), H - ra)
    cb = (R_END - rb) / (rb + R_POCKET)
    b1 = nang + math.degrees(math.acos(cb))
    b2 = nang - math.degrees(math.acos(cb))
    beta = b1 if math.cos(math.radians(b1)) > math.cos(math.radians(b2)) else b2
    B = _on((CY, CZ), rb + R_POCKET, beta)
    ang_ga = math.degrees(math.atan2(A[1] - CZ, A[0] - CY))
    ta = _on((CY, CZ), R_POCKET, ang_ga)
    tb = _on((CY, CZ), R_POCKET, beta)
    ang_a = ang_ga + 180.0
    ang_b = beta + 180.0
    while ang_b > nang:
        ang_b -= 360.0
    f_diag = _on(F, R_BL, nang)
    b_diag = _on(B, rb, nang)
    segs = [
        ("line", (A[0], H), (tr[0], H), None),
        ("arc", (tr[0], H), (L, tr[1]), _on(tr, R_TR, 45)),
        ("line", (L, tr[1]), (L, br[1]), None),
        ("arc", (L, br[1]), (br[0], 0.0), _on(br, R_BR, -45)),
        ("line", (br[0], 0.0), (F[0], 0.0), None),
        ("arc", (F[0], 0.0), f_diag, _on(F, R_BL, (-90 + nang) / 2.0)),
        ("line", f_diag, b_diag, None),
        ("arc", b_diag, tb, _on(B, rb, (nang + ang_b) / 2.0)),
        ("arc", tb, ta, _on((CY, CZ), R_POCKET, (beta + ang_ga) / 2.0)),
        ("arc", ta, (A[0], H), _on(A, ra, (ang_a + 90.0) / 2.0)),
    ]
    # edge radius at each outline vertex (linear in between)
    vr = [((A[0], H), COVER_EDGE_BIG),
          ((tr[0], H), COVER_EDGE_SMALL), ((L, tr[1]), COVER_EDGE_SIDE),
          ((L, br[1]), COVER_EDGE_SIDE), ((br[0], 0.0), COVER_EDGE_SMALL),
          ((F[0], 0.0), COVER_EDGE_BL),
          (f_diag, COVER_EDGE_BL), (b_diag, COVER_EDGE_ARCB),
          (tb, COVER_EDGE_ARCB), (ta, COVER_EDGE_BIG)]
    return segs, vr


cover_segs, cover_vr = cover_geometry()
wp = yz(X_RIM).moveTo(*cover_segs[0][1])
for kind, p0, p1, pm in cover_segs:
    wp = wp.lineTo(*p1) if kind == "line" else wp.threePointArc(pm, p1)
cover = wp.close().extrude(X_COVER - X_RIM, clean=False)


def cover_radius_fn(rmin):
    def f(p):
        best = min(cover_vr, key=lambda v: (v[0][0] - p.y) ** 2 + (v[0][1] - p.z) ** 2)
        return max(best[1], rmin)
    return f


cover_raw = cover
for rmin in (0.0, 2.5, 4.0):
    try:
        cover = variable_fillet(cover_raw, cover_raw.faces(">X").edges().vals()[0], cover_radius_fn(rmin))
        break
    except Exception:
        cover = None
if cover is None:
    cover = cover_raw.faces(">X").edges().fillet(COVER_EDGE_SMALL)

body = back.union(cover)

# ---------------- drum with bolt circle and central hex ----------------
drum = yz(X_FLOOR - 0.01).center(CY, CZ).circle(R_DRUM).extrude(X_DRUM - X_FLOOR + 0.01)
drum = drum.faces(">X").edges().chamfer(DRUM_CHAMFER)
body = body.union(drum)

bolts = (yz(X_DRUM - 0.01).center(CY, CZ)
         .polarArray(R_BOLTS, 0, 360, N_BOLTS).polygon(6, BOLT_AF).extrude(1.0))
body = body.union(bolts)
hexplate = (yz(X_DRUM - 0.01).center(CY, CZ).transformed(rotate=(0, 0, 90))
            .polygon(6, HEX_PLATE).extrude(HEX_PLATE_T + 0.01))
nut = yz(X_DRUM + HEX_PLATE_T).center(CY, CZ).polygon(6, HEX_NUT).extrude(HEX_NUT_T)
body = body.union(hexplate).union(nut)
body = body.cut(yz(X_DRUM - 3).center(CY, CZ).circle(BORE_R).extrude(10))

# strap slot in the bottom-left diagonal face (below the rim)
_n, _nang, _F = _diag()
_sy = CY + (R_END - (SLOT2_Z - CZ) * _n[1]) / _n[0]          # point on the diagonal
_orig = cq.Vector(SLOT2_X, _sy + _n[0] * 1.0, SLOT2_Z + _n[1] * 1.0)
_pl = cq.Plane(origin=_orig, xDir=(1, 0, 0), normal=(0, -_n[0], -_n[1]))
body = body.cut(cq.Workplane(_pl).slot2D(SLOT2_LEN, SLOT2_W).extrude(SLOT2_DEPTH + 1.0))

# small screw heads on the rim
for (py, pz) in RIM_SCREWS:
    body = body.union(yz(X_RIM - 0.01).center(py, pz).polygon(6, 2.6).extrude(1.0))

# screw holes through the cover
for (py, pz) in COVER_HOLES:
    body = body.cut(yz(X_COVER - 10).center(py, pz).circle(COVER_HOLE_R).extrude(20))

# ---------------- splined plug shaft on +Y ----------------
def shaft_wp(y):
    return cq.Workplane("XZ", origin=(0, y, 0)).center(SHAFT_X, CZ)


shaft = shaft_wp(L - 2).circle(SHAFT_R).extrude(-(SHAFT_LEN + 2))
shaft = shaft.faces(">Y").edges().chamfer(0.6)
for i in range(N_RIBS):
    y0 = L + COLLAR_LEN + 1.0 + i * RIB_PITCH
    rib = shaft_wp(y0).circle(RIB_R).extrude(-RIB_W)
    rib = rib.faces("<Y or >Y").edges().chamfer(0.5)
    shaft = shaft.union(rib)
shaft = shaft.cut(shaft_wp(L + SHAFT_LEN + 1).circle(SHAFT_BORE).extrude(SHAFT_LEN - COLLAR_LEN + 1))
slot = cq.Workplane("XY").box(2 * RIB_R + 4, SLOT_Y1 - SLOT_Y0, SLOT_W).translate(
    (SHAFT_X, (SLOT_Y0 + SLOT_Y1) / 2, CZ))
shaft = shaft.cut(slot)
body = body.union(shaft)

result = body.translate((-X_COVER / 2, -L / 2, -H / 2))
